import math
import cadquery as cq

# Modular speed-bump / speed-cushion segment: an arched slab (crown along Y),
# interlocking tabs on the -X side, matching notches on the +X side,
# six counterbored fixing holes and six shallow reflector recesses on top.

# ---------------- driving dimensions (mm) ----------------
L = 900.0          # length along Y (direction of the arched profile)
W = 500.0          # width along X
H = 50.0           # crown height at the centre
NOSE_R = 3.0       # radius of the rounded nose at both ends

# interlocking tabs (-X side) and notches (+X side)
TAB_Y = 180.0      # |y| of tab / notch centre
TAB_W = 40.0       # tab / notch width along Y
TAB_D = 25.0       # tab protrusion / notch depth along X

# fixing holes (counterbored)
HOLE_X = 171.0
HOLE_Y = (-400.0, 0.0, 400.0)
CB_D = 38.0        # counterbore diameter
CB_DEPTH = 3.0     # counterbore floor below the lowest point of its rim
THRU_D = 6.5       # through hole diameter

# shallow rectangular recesses on the top (reflector panels)
REC_W = 255.0                      # along X
REC_L = 100.0                      # along Y
REC_Y = (80.0, 220.0, 360.0)       # |y| of panel centres (mirrored about y=0)
REC_DEPTH = 0.3

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- crown geometry ----------------
# big circular crown arc through (0,H), internally tangent to the two nose
# circles of radius NOSE_R centred at (+-(L/2-NOSE_R), 0)
R = ((L / 2 - NOSE_R) ** 2 + H ** 2 - NOSE_R ** 2) / (2 * (H - NOSE_R))
CZ = H - R                                  # z of the crown arc centre
_NC = L / 2 - NOSE_R                        # |y| of nose circle centres
_D = math.hypot(_NC, -CZ)
_UY, _UZ = _NC / _D, -CZ / _D               # unit vector crown centre -> nose centre
TP_Y, TP_Z = _NC + NOSE_R * _UY, NOSE_R * _UZ   # tangent point (|y|, z)
_AM = 0.5 * (0.0 + math.atan2(_UZ, _UY))   # mid angle on the nose arc
NM_Y, NM_Z = _NC + NOSE_R * math.cos(_AM), NOSE_R * math.sin(_AM)


def crown_z(y):
    """height of the top surface at position y (crown region)"""
    return CZ + math.sqrt(R * R - y * y)


def arch(x0, x1):
    """arched profile (in the YZ plane) extruded from x = x0 to x = x1:
    rounded nose - circular crown - rounded nose, all tangent"""
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .moveTo(-L / 2, 0)
        .lineTo(L / 2, 0)
        .threePointArc((NM_Y, NM_Z), (TP_Y, TP_Z))
        .threePointArc((0, H), (-TP_Y, TP_Z))
        .threePointArc((-NM_Y, NM_Z), (-L / 2, 0))
        .close()
        .extrude(x1 - x0)
    )


def box(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0))
    )


# ---------------- main body ----------------
# one extrusion over the full width including the tab zone, so that the
# tabs share the crown surface, then remove the tab zone except the tabs
body = arch(-W / 2 - TAB_D, W / 2)
tab_zone = box(-W / 2 - TAB_D - 5, -W / 2, -L / 2 - 5, L / 2 + 5, -5, H + 5)
for s in (-1, 1):
    yc = s * TAB_Y
    tab_zone = tab_zone.cut(
        box(-W / 2 - TAB_D - 10, -W / 2 + 5, yc - TAB_W / 2, yc + TAB_W / 2, -10, H + 10)
    )
body = body.cut(tab_zone)

# matching notches on the +X side
for s in (-1, 1):
    yc = s * TAB_Y
    body = body.cut(
        box(W / 2 - TAB_D, W / 2 + 5, yc - TAB_W / 2, yc + TAB_W / 2, -5, H + 5)
    )

# ---------------- shallow recessed panels ----------------
skin = arch(-W / 2 - 10, W / 2 + 10).cut(
    arch(-W / 2 - 10, W / 2 + 10).translate((0, 0, -REC_DEPTH))
)
for s in (-1, 1):
    for yc in REC_Y:
        win = box(-REC_W / 2, REC_W / 2, s * yc - REC_L / 2, s * yc + REC_L / 2, -5, H + 5)
        body = body.cut(skin.intersect(win))

# ---------------- counterbored fixing holes ----------------
for hx in (-HOLE_X, HOLE_X):
    for hy in HOLE_Y:
        z_floor = crown_z(abs(hy) + CB_D / 2) - CB_DEPTH
        cb = (
            cq.Workplane("XY", origin=(hx, hy, z_floor))
            .circle(CB_D / 2)
            .extrude(H + 10)
        )
        th = (
            cq.Workplane("XY", origin=(hx, hy, -5))
            .circle(THRU_D / 2)
            .extrude(H + 20)
        )
        body = body.cut(cb).cut(th)

result = body
